import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 5.9              # body thickness
HEAD_R = 24.2        # radius of each head disc
HEAD_X = 75.6        # head centre distance from middle along X
HEAD_R_DY = -4.1     # right head centre offset in Y (left head on handle axis)
HANDLE_HW = 8.3      # handle half width
NECK_R = 53.5        # big concave blend radius handle -> head
JAW_W = 25.8         # jaw opening (across flats)
JAW_ANG = 17.0       # jaw axis angle w.r.t. the handle (deg)
THROAT_R = 16.9      # throat arc radius
THROAT_BACK = 10.9   # throat arc centre behind head centre (along jaw axis)
THROAT_FIL = 1.0     # fillet where throat meets the jaw flats
TIP_FIL = 0.8        # rounding of the jaw tips
EDGE_FIL = 0.6       # perimeter edge rounding (top and bottom)

# shallow grip recess on both faces of the handle
REC_D = 0.7          # recess depth
REC_FLOOR_FIL = 0.35 # floor fillet of the recess
REC_CORNER = 1.3     # plan-view corner radius
REC_HW = 3.85        # recess half width in the middle
REC_L = 91.0         # recess overall length

VIEW = {"azimuth": 45, "elevation": 26}


def _unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def neck_fillet(hc, side, sign_y):
    """Concave blend between handle edge y = sign_y*HANDLE_HW and head circle.
    side = -1 for left head, +1 for right head.
    Returns (point on handle line, arc mid point, point on head circle)."""
    xh, yh = hc
    fy = sign_y * (HANDLE_HW + NECK_R)
    dy = fy - yh
    dx = math.sqrt((HEAD_R + NECK_R) ** 2 - dy ** 2)
    fx = xh - side * dx
    t1 = (fx, sign_y * HANDLE_HW)
    d = _unit((fx - xh, fy - yh))
    t2 = (xh + HEAD_R * d[0], yh + HEAD_R * d[1])
    a = _unit((t1[0] - fx, t1[1] - fy))
    b = _unit((t2[0] - fx, t2[1] - fy))
    m = _unit((a[0] + b[0], a[1] + b[1]))
    mid = (fx + NECK_R * m[0], fy + NECK_R * m[1])
    return t1, mid, t2


def rounded_polygon(wp, pts, radii):
    """Closed polygon with every corner rounded by its own radius (lines + arcs)."""
    n = len(pts)
    corners = []
    for i in range(n):
        p = pts[i]
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        d1 = _unit((a[0] - p[0], a[1] - p[1]))
        d2 = _unit((b[0] - p[0], b[1] - p[1]))
        cosang = max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1]))
        half = math.acos(cosang) / 2.0
        r = radii[i]
        t = r / math.tan(half)
        t1 = (p[0] + d1[0] * t, p[1] + d1[1] * t)
        t2 = (p[0] + d2[0] * t, p[1] + d2[1] * t)
        bis = _unit((d1[0] + d2[0], d1[1] + d2[1]))
        h = r / math.sin(half)
        c = (p[0] + bis[0] * h, p[1] + bis[1] * h)
        m = (c[0] - bis[0] * r, c[1] - bis[1] * r)
        corners.append((t1, m, t2))
    w = wp.moveTo(*corners[0][2])
    for i in range(1, n + 1):
        t1, m, t2 = corners[i % n]
        w = w.lineTo(*t1).threePointArc(m, t2)
    return w.close()


HL = (-HEAD_X, 0.0)
HR = (HEAD_X, HEAD_R_DY)

ul = neck_fillet(HL, -1, +1)
ll = neck_fillet(HL, -1, -1)
ur = neck_fillet(HR, +1, +1)
lr = neck_fillet(HR, +1, -1)

# ---------------- plan outline, extruded ----------------
outline = (
    cq.Workplane("XY")
    .moveTo(*ul[0])
    .lineTo(*ur[0])
    .threePointArc(ur[1], ur[2])
    .threePointArc((HR[0] + HEAD_R, HR[1]), lr[2])
    .threePointArc(lr[1], lr[0])
    .lineTo(*ll[0])
    .threePointArc(ll[1], ll[2])
    .threePointArc((HL[0] - HEAD_R, HL[1]), ul[2])
    .threePointArc(ul[1], ul[0])
    .close()
)
body = outline.extrude(T).translate((0, 0, -T / 2)).val()


# ---------------- jaw cut-outs ----------------
def to_world(hc, ang_deg, u, v):
    c, s = math.cos(math.radians(ang_deg)), math.sin(math.radians(ang_deg))
    return (hc[0] + u * c - v * s, hc[1] + u * s + v * c)


def jaw_cutter(hc, ang_deg):
    """Open-end jaw: parallel flats, arc throat.  Local u runs along the inward jaw axis."""
    L = HEAD_R * 3
    band = cq.Workplane("XY").box(L, JAW_W, T * 3, centered=(False, True, True)).translate(
        (-L + (-THROAT_BACK + THROAT_R), 0, 0)
    )
    straight = cq.Workplane("XY").box(L, JAW_W * 2, T * 3, centered=(False, True, True)).translate(
        (-L - THROAT_BACK, 0, 0)
    )
    disc = cq.Workplane("XY").circle(THROAT_R).extrude(T * 3).translate((-THROAT_BACK, 0, -T * 1.5))
    cut = band.intersect(straight.union(disc))
    return cut.rotate((0, 0, 0), (0, 0, 1), ang_deg).translate((hc[0], hc[1], 0)).val()


jaws = [(HL, JAW_ANG), (HR, JAW_ANG + 180.0)]
for hc, ang in jaws:
    body = body.cut(jaw_cutter(hc, ang))


def vertical_edges_near(shape, pts, tol=0.5):
    out = []
    for e in shape.Edges():
        bb = e.BoundingBox()
        if bb.zlen < T * 0.9:
            continue
        c = e.Center()
        for p in pts:
            if math.hypot(c.x - p[0], c.y - p[1]) < tol:
                out.append(e)
                break
    return out


u_throat = -THROAT_BACK + math.sqrt(THROAT_R ** 2 - (JAW_W / 2) ** 2)
u_tip = -math.sqrt(HEAD_R ** 2 - (JAW_W / 2) ** 2)
throat_pts, tip_pts = [], []
for hc, ang in jaws:
    for v in (JAW_W / 2, -JAW_W / 2):
        throat_pts.append(to_world(hc, ang, u_throat, v))
        tip_pts.append(to_world(hc, ang, u_tip, v))

body = body.fillet(THROAT_FIL, vertical_edges_near(body, throat_pts))
body = body.fillet(TIP_FIL, vertical_edges_near(body, tip_pts))

# perimeter rounding on the top and bottom faces
rim = [
    e
    for e in body.Edges()
    if e.BoundingBox().zlen < 1e-3 and abs(abs(e.Center().z) - T / 2) < 1e-3
]
body = body.fillet(EDGE_FIL, rim)

# ---------------- shallow grip recess on both faces ----------------
hl = REC_L / 2.0
FL = REC_HW + 3.15  # flared half width at the left end (+Y side)
rec_pts = [
    (-hl + 1.6, -REC_HW - 0.6),    # bottom-left corner
    (-hl + 11.5, -REC_HW),         # end of small left flare
    (hl - 11.5, -REC_HW),          # start of small right flare
    (hl - 1.9, -REC_HW - 0.65),    # bottom-right corner
    (hl - 0.2, -1.6),              # right end, lower
    (hl + 0.0, 2.2),               # right end, upper
    (hl - 2.9, REC_HW + 1.45),     # top-right corner
    (hl - 10.0, REC_HW),           # start of right flare
    (-hl + 16.5, REC_HW),          # start of left (swept) flare
    (-hl + 3.3, FL),               # top-left flared corner
    (-hl - 0.4, -1.0),             # left end tip
]
rc = REC_CORNER
rec_r = [rc, 8.0, 8.0, rc, 1.5, 1.5, rc, 6.0, 30.0, 2.0, 2.0]

for sgn in (+1, -1):
    tool = rounded_polygon(cq.Workplane("XY"), rec_pts, rec_r).extrude(REC_D + 2.0)
    # tool spans z in [0, REC_D+2]; round the floor edges then place it
    tool = tool.faces("<Z").edges().fillet(REC_FLOOR_FIL)
    if sgn > 0:
        tool = tool.translate((0, 0, T / 2 - REC_D))
    else:
        tool = tool.mirror("XY").translate((0, 0, -T / 2 + REC_D))
    body = body.cut(tool.val())

solids = body.Solids()
result = cq.Workplane("XY").newObject([solids[0] if len(solids) == 1 else body])
